import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 200.0        # width  (X)
H = 300.0        # height (Z)
D = 75.0         # depth  (Y), closed face at -Y, open at +Y
T_WALL = 16.0    # side / top / bottom wall thickness
T_FRONT = 11.0   # closed front plate thickness
R_EDGE = 2.0     # outer edge fillet

# corner lid-screw holes (through the full depth) with hex nut traps on the front
CORNER_OFF_X = 9.2
CORNER_OFF_Z = 9.0
CORNER_HOLE_D = 7.0
HEX_AF = 12.6
HEX_DEPTH = 6.0     # nut-trap depth into the front plate

# front plate mounting holes (x, z)
FRONT_HOLE_D = 6.5
PAT_A = ((-73.5, -19.0), (-21.2, -125.3))    # x pair, z pair
PAT_B = ((3.5, 72.8), (-23.1, -123.2))
FRONT_HOLES = [(x, z) for (xs, zs) in (PAT_A, PAT_B) for x in xs for z in zs]

# side (+X) gland hole with rounded rim
SIDE_HOLE_D = 10.5
SIDE_HOLE_R = 1.75
SIDE_HOLE_Z = 19.0
SIDE_HOLE_Y = -5.6

# bottom through slots (x0, x1, y0, y1) with rounded outer rims
BIG_SLOT = (-4.4, 80.0, -17.5, 9.5)
SMALL_SLOT = (-63.0, -31.2, -26.8, -10.4)
SLOT_R = 1.5

# ---------------- body ----------------
body = cq.Workplane("XY").box(W, D, H).edges().fillet(R_EDGE)

cavity = (cq.Workplane("XY")
          .box(W - 2 * T_WALL, D - T_FRONT + 1.0, H - 2 * T_WALL)
          .translate((0, (T_FRONT + 1.0) / 2.0, 0)))
body = body.cut(cavity)

# side hole through +X wall, rim rounded
side = (cq.Workplane("YZ", origin=(W / 2 + 1, 0, 0))
        .center(SIDE_HOLE_Y, SIDE_HOLE_Z).circle(SIDE_HOLE_D / 2)
        .extrude(-(T_WALL + 2)))
body = body.cut(side)
body = body.edges(cq.selectors.BoxSelector(
    (W / 2 - 0.5, SIDE_HOLE_Y - SIDE_HOLE_D, SIDE_HOLE_Z - SIDE_HOLE_D),
    (W / 2 + 0.5, SIDE_HOLE_Y + SIDE_HOLE_D, SIDE_HOLE_Z + SIDE_HOLE_D))).fillet(SIDE_HOLE_R)

# bottom through slots, outer rim rounded
zb = -H / 2
for (x0, x1, y0, y1) in (BIG_SLOT, SMALL_SLOT):
    slot = (cq.Workplane("XY", origin=(0, 0, zb - 1))
            .center((x0 + x1) / 2, (y0 + y1) / 2)
            .rect(x1 - x0, y1 - y0).extrude(T_WALL + 2))
    body = body.cut(slot)
    body = body.edges(cq.selectors.BoxSelector(
        (x0 - 0.5, y0 - 0.5, zb - 0.5), (x1 + 0.5, y1 + 0.5, zb + 0.5))).fillet(SLOT_R)

# corner through holes along Y and hex pockets on the front face
cx = W / 2 - CORNER_OFF_X
cz = H / 2 - CORNER_OFF_Z
corner_pts = [(sx * cx, sz * cz) for sx in (-1, 1) for sz in (-1, 1)]
for (x, z) in corner_pts:
    hole = (cq.Workplane("XZ", origin=(0, D / 2 + 1, 0))
            .center(x, z).circle(CORNER_HOLE_D / 2).extrude(D + 2))
    body = body.cut(hole)
    hexp = (cq.Workplane("XZ", origin=(0, -D / 2, 0))
            .center(x, z)
            .polygon(6, HEX_AF / 0.8660254)
            .extrude(-HEX_DEPTH))
    hexp = hexp.rotate((x, 0, z), (x, 1, z), 30)
    body = body.cut(hexp)

# front plate holes
for (x, z) in FRONT_HOLES:
    hole = (cq.Workplane("XZ", origin=(0, -D / 2 - 1, 0))
            .center(x, z).circle(FRONT_HOLE_D / 2).extrude(-(T_FRONT + 2)))
    body = body.cut(hole)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
